import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 500.0          # overall length (Y)
W = 88.0           # overall width  (X)
H = 47.5           # body height    (Z)
CH = 29.0          # 45 deg chamfer on the +X end corners
R_V = 3.5          # vertical edge fillet

SLOT_Y = 116.5     # slot centre distance from middle
SLOT_W = 32.0      # slot width
SLOT_WALL = 3.0    # material left at the +X side of the slot

# underside pocketing
TOP_T = 10.5       # top skin thickness
XW_IN = -35.0      # inner face of the -X wall
XE_IN = 28.5       # inner face of the +X wall
RIB = 11.0         # diagonal rib thickness (middle block)
RIB_END = 10.0     # diagonal rib thickness (end blocks)
WALL_Y = 9.5       # slot side wall thickness
END_WALL = 9.5     # end wall thickness
POCKET_R = 3.0     # pocket corner radius
BOSS_D = 10.0
BOSS_X = XW_IN + BOSS_D / 2 - 1.0

# central trapezoid (|Y| <= TRAP_C - X), open to the top for X >= TRAP_X0
TRAP_C = 42.5
TRAP_X0 = -5.4

# L-brackets
BR_LEG_T = 6.0
BR_LEG_X0 = -14.6  # -X face of vertical leg
BR_FL_T = 2.0      # flange thickness
BR_H = 30.4        # leg height above body top
END_BR_LEN = 70.0
END_BR_SLOPE = 29.0
MID_BR_LEN = 108.0

HOLE_SIDE_D = 9.0
HOLE_SIDE_Z = 22.0
HOLE_SIDE_DEPTH = 13.0
SIDE_HOLES_Y = (20.0, 145.5, 185.0)
HOLE_PLATE_D = 7.0
HOLE_PLATE_Z = 15.3   # above body top
HOLE_FL_D = 5.5
FL_HOLE_DEPTH = 8.0   # into the body below the flange
FL_HOLE_X = -29.5
END_FL_HOLE_Y = L / 2 - 63.0
MID_FL_HOLE_Y = 32.6

# cable tie mounts
CT_X = (30.0, 40.0)
CT_W = 4.0
CT_LEN = 13.0
CT_H = 3.0
CT_Y = 59.5

VIEW = {"azimuth": 45, "elevation": 26}

TOPZ = H


def body_outline():
    pts = [
        (-W / 2, -L / 2),
        (W / 2 - CH, -L / 2),
        (W / 2, -L / 2 + CH),
        (W / 2, L / 2 - CH),
        (W / 2 - CH, L / 2),
        (-W / 2, L / 2),
    ]
    return cq.Workplane("XY").polyline(pts).close()


def prism(pts, z0, z1, r=None):
    wp = cq.Workplane("XY").workplane(offset=z0).polyline(pts).close().extrude(z1 - z0)
    if r:
        wp = wp.edges("|Z").fillet(r)
    return wp


def mirror_y(pts):
    return [(x, -y) for (x, y) in reversed(pts)]


body = body_outline().extrude(H)
body = body.edges("|Z").fillet(R_V)

# ---------------- underside pockets ----------------
pz1 = H - TOP_T
pockets = []
# middle block
yi_mid = SLOT_Y - SLOT_W / 2 - WALL_Y          # slot-side inner face
c_rib = TRAP_C + RIB * 2 ** 0.5                 # diag rib far side
central = [(XE_IN, -(TRAP_C - XE_IN)), (XE_IN, TRAP_C - XE_IN),
           (XW_IN, TRAP_C - XW_IN), (XW_IN, -(TRAP_C - XW_IN))]
pockets.append(central)
tri1 = [(c_rib - yi_mid, -yi_mid), (XE_IN, -yi_mid), (XE_IN, XE_IN - c_rib)]
pockets.append(tri1)
pockets.append(mirror_y(tri1))

# end blocks (built for -Y end, mirrored)
y_end_in = -L / 2 + END_WALL
y_slot_in = -(SLOT_Y + SLOT_W / 2) - WALL_Y
ch_c = (W / 2 - CH) + L / 2 - END_WALL * 2 ** 0.5   # X - Y <= ch_c (wall along the chamfer)
y_rib0 = -218.5
y_rib1 = y_rib0 + 11.0
p1 = [(XW_IN, y_end_in), (ch_c + y_end_in, y_end_in), (ch_c + y_rib0, y_rib0), (XW_IN, y_rib0)]
d2 = -185.0                                   # X + Y <= d2
p2 = [(XW_IN, y_rib1), (d2 - y_rib1, y_rib1), (XW_IN, d2 - XW_IN)]
d3 = d2 + RIB_END * 2 ** 0.5
p3 = [(d3 - y_slot_in, y_slot_in), (XE_IN, d3 - XE_IN), (XE_IN, y_slot_in)]
for p in (p1, p2, p3):
    pockets.append(p)
    pockets.append(mirror_y(p))

for p in pockets:
    body = body.cut(prism(p, -1.0, pz1, POCKET_R))

# open the central trapezoid through the top skin
trap_top = [(TRAP_X0, -(TRAP_C - TRAP_X0)), (XE_IN, -(TRAP_C - XE_IN)),
            (XE_IN, TRAP_C - XE_IN), (TRAP_X0, TRAP_C - TRAP_X0)]
body = body.cut(prism(trap_top, pz1 - 1, H + 1))

# bosses under the flange holes
for (bx, by) in [(BOSS_X, -END_FL_HOLE_Y), (BOSS_X, END_FL_HOLE_Y),
                 (BOSS_X, -MID_FL_HOLE_Y), (BOSS_X, MID_FL_HOLE_Y)]:
    boss = cq.Workplane("XY").center(bx, by).circle(BOSS_D / 2).extrude(pz1 + 0.5)
    body = body.union(boss)

# ---------------- U slots from the -X side ----------------
for sy in (-SLOT_Y, SLOT_Y):
    x_end = W / 2 - SLOT_WALL - SLOT_W / 2
    x_st = -W / 2 - 20
    slot = (
        cq.Workplane("XY").workplane(offset=-1)
        .center((x_end + x_st) / 2, sy)
        .slot2D(x_end - x_st + SLOT_W, SLOT_W, 0)
        .extrude(H + 2)
    )
    body = body.cut(slot)

# round the slot entry corners on the -X face
SLOT_EDGE_R = 3.5
corner_pts = [(-W / 2, sy * (SLOT_Y + d)) for sy in (-1, 1) for d in (-SLOT_W / 2, SLOT_W / 2)]
sel = []
for e in body.edges("|Z").vals():
    c = e.Center()
    if any(abs(c.x - px) < 0.3 and abs(c.y - py) < 0.3 for (px, py) in corner_pts):
        sel.append(e)
body = body.newObject(sel).fillet(SLOT_EDGE_R)

result = body

# ---------------- L-brackets ----------------
FL_X0 = -W / 2
FL_X1 = BR_LEG_X0 + BR_LEG_T


outline_cap = (body_outline().extrude(BR_FL_T).edges("|Z").fillet(R_V)
               .translate((0, 0, TOPZ)))


def flange(y0, y1):
    blk = (cq.Workplane("XY").workplane(offset=TOPZ)
           .center((FL_X0 + FL_X1) / 2, (y0 + y1) / 2)
           .rect(FL_X1 - FL_X0, y1 - y0).extrude(BR_FL_T))
    return blk.intersect(outline_cap)


def leg_profile(pts):
    # pts in (Y, Z); extruded along +X by the leg thickness
    wp = cq.Workplane("YZ", origin=(BR_LEG_X0, 0, 0)).polyline(pts).close()
    return wp.extrude(BR_LEG_T)


for s in (-1, 1):
    yend = s * L / 2
    yin = s * (L / 2 - END_BR_LEN)
    ysl = s * (L / 2 - END_BR_SLOPE)
    fl = flange(min(yend, yin), max(yend, yin))
    pts = [(yend, TOPZ), (yin, TOPZ), (yin, TOPZ + BR_H), (ysl, TOPZ + BR_H), (yend, TOPZ + BR_FL_T)]
    result = result.union(fl).union(leg_profile(pts))

fl = flange(-MID_BR_LEN / 2, MID_BR_LEN / 2)
leg = leg_profile([(-MID_BR_LEN / 2, TOPZ), (MID_BR_LEN / 2, TOPZ),
                   (MID_BR_LEN / 2, TOPZ + BR_H), (-MID_BR_LEN / 2, TOPZ + BR_H)])
result = result.union(fl).union(leg)

# ---------------- cable tie mounts ----------------
for sy in (-CT_Y, CT_Y):
    for cx in CT_X:
        blk = (cq.Workplane("XY").workplane(offset=TOPZ).center(cx, sy)
               .rect(CT_W, CT_LEN).extrude(CT_H))
        gap = (cq.Workplane("XY").workplane(offset=TOPZ - 0.1).center(cx, sy)
               .rect(CT_W + 2, CT_LEN - 4).extrude(CT_H - 1.0 + 0.1))
        result = result.union(blk.cut(gap))

# ---------------- holes ----------------
def x_hole(x0, length, y, z, d):
    # cylinder along +X; its seam is turned away from the default camera
    cyl = cq.Solid.makeCylinder(d / 2, length, cq.Vector(x0, y, z), cq.Vector(1, 0, 0))
    cyl = cyl.rotate(cq.Vector(x0, y, z), cq.Vector(x0 + 1, y, z), 135)
    return cq.Workplane("XY").add(cyl)


# side holes in the +X face
for y in SIDE_HOLES_Y:
    for sy in (-y, y):
        result = result.cut(x_hole(W / 2 - HOLE_SIDE_DEPTH, HOLE_SIDE_DEPTH + 1, sy, HOLE_SIDE_Z, HOLE_SIDE_D))

# holes through the bracket legs
for y in (-(L / 2 - END_BR_LEN / 2), 0.0, L / 2 - END_BR_LEN / 2):
    result = result.cut(x_hole(BR_LEG_X0 - 1, BR_LEG_T + 2, y, TOPZ + HOLE_PLATE_Z, HOLE_PLATE_D))

# flange holes
for y in (-END_FL_HOLE_Y, END_FL_HOLE_Y, -MID_FL_HOLE_Y, MID_FL_HOLE_Y):
    h = (cq.Workplane("XY").workplane(offset=TOPZ - FL_HOLE_DEPTH).center(FL_HOLE_X, y)
         .circle(HOLE_FL_D / 2).extrude(FL_HOLE_DEPTH + BR_FL_T + 1))
    result = result.cut(h)
